import cadquery as cq

# Hollow dome cap: truncated sphere with a spherical "nipple" on top, blended by a
# concave fillet, shelled to a uniform wall, open flat bottom, and four radial
# through holes just above the rim.

# ---------------- driving dimensions (mm) ----------------
R_MAIN = 50.0        # radius of the main spherical dome (sphere centre = origin)
Z_BOTTOM = -16.35    # flat open bottom plane (below the sphere centre)
R_BUMP = 31.3        # radius of the top bump sphere
Z_BUMP = 25.95       # height of the bump sphere centre above the main centre
F_NECK = 2.5         # concave fillet between dome and bump
WALL = 3.4           # uniform wall thickness
HOLE_D = 7.1         # radial through holes near the rim
HOLE_H = 8.55        # hole axis height above the flat rim
N_HOLES = 4          # equally spaced, first one on +X
HOLE_START = 0.0     # azimuth of the first hole (deg)

# where the (tessellation-visible) parametric seams of the spheres are put
SEAM_OUT = 135.0     # outer dome seam meridian: back-left side
SEAM_IN = -45.0      # cavity seam meridian: hidden behind the near wall

BIG = 4.0 * R_MAIN


def sphere(radius, zc, seam_az=0.0, horizontal_axis=False):
    """Full sphere centred on the Z axis at height zc.
    seam_az         : azimuth of the seam meridian (vertical polar axis).
    horizontal_axis : lay the polar axis along X so the seam runs under the
                      sphere (used for the bump, whose underside is buried)."""
    s = cq.Solid.makeSphere(radius, angleDegrees1=-90, angleDegrees2=90)
    if horizontal_axis:
        s = s.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 90)
    else:
        s = s.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), seam_az)
    return cq.Workplane("XY").add(s.translate(cq.Vector(0, 0, zc)))


def junction_z(r_a, r_b, zc_b):
    """Height of the intersection circle of sphere(r_a, origin) and sphere(r_b, zc_b)."""
    return (r_a ** 2 - r_b ** 2 + zc_b ** 2) / (2.0 * zc_b)


def dome(r_main, r_bump, fillet_r, seam_az, bump_horizontal):
    """Main sphere + bump sphere, joined by a concave fillet along their junction."""
    body = sphere(r_main, 0.0, seam_az).union(
        sphere(r_bump, Z_BUMP, seam_az, horizontal_axis=bump_horizontal))
    zj = junction_z(r_main, r_bump, Z_BUMP)
    neck = body.edges(cq.selectors.BoxSelector((-BIG, -BIG, zj - 2.0), (BIG, BIG, zj + 2.0)))
    return neck.fillet(fillet_r)


# outer skin, and the cavity as its exact inward offset (uniform wall)
outer = dome(R_MAIN, R_BUMP, F_NECK, SEAM_OUT, True)
cavity = dome(R_MAIN - WALL, R_BUMP - WALL, F_NECK + WALL, SEAM_IN, False)

# truncate with the flat bottom plane and hollow out
below = cq.Workplane("XY").box(BIG, BIG, BIG).translate((0, 0, Z_BOTTOM - BIG / 2.0))
part = outer.cut(below).cut(cavity)

# polar pattern of radial through holes (drilled from the axis outwards)
z_hole = Z_BOTTOM + HOLE_H
for i in range(N_HOLES):
    ang = HOLE_START + 360.0 * i / N_HOLES
    drill = (cq.Workplane("YZ").circle(HOLE_D / 2.0).extrude(R_MAIN + 10.0)
             .translate((0, 0, z_hole))
             .rotate((0, 0, 0), (0, 0, 1), ang))
    part = part.cut(drill)

result = part

VIEW = {"azimuth": 45, "elevation": 26}
